import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Linkage bracket: a short rectangular tube (axis along Y) carrying a planar
# six-link mechanism on each side wall (+X and -X).  Every link is a flat
# "stadium" plate lying in a YZ plane; on each side the links sit in two
# layers (inner layer on the tube wall, outer layer on top of it).
# The box and the ten links are separate bodies (an assembled mechanism).
#
# Each side:  upper arm  (top wall pivot  -> tip, hole at 2/3)
#             lower arm  (bottom pivot   -> tip, hole at 2/3 or 1/3)
#             rocker     (middle pivot   -> joint J)           inner layer
#             coupler 1  (upper arm hole -> J)                 outer layer
#             coupler 2  (J -> lower arm hole)                 outer layer
# The joint positions are solved from the link lengths (circle-circle
# intersections), so changing a length or a pose angle keeps it assembled.
# ---------------------------------------------------------------------------

# --- box (rectangular tube, open along Y) ---
BOX_W = 91.5      # X, outer
BOX_D = 27.0      # Y, tube length
BOX_H = 121.0     # Z, outer
WALL = 7.8        # wall thickness

# --- links ---
LINK_T = 7.8      # plate thickness (X)
LINK_R = 9.3      # half width = end radius
HOLE_R = 5.2      # pivot hole radius

PIVOT_DZ = 45.4                 # spacing of the three pivots on a side wall
L_LONG = 113.6                  # arm length, pivot to tip
L_HOLE = L_LONG * 2.0 / 3.0     # intermediate hole on an arm
L_MID = 90.8                    # coupler length
L_SHORT = 15.2                  # rocker length

# pose of each mechanism: upper-arm angle in the YZ plane, from +Y toward +Z
THETA_POS_X = 25.6    # +X side, arm reaches toward +Y
THETA_NEG_X = 160.7   # -X side, arm reaches toward -Y

# pivots on the side walls (Y, Z)
TOP = (0.0, PIVOT_DZ)
MID = (0.0, 0.0)
BOT = (0.0, -PIVOT_DZ)


def circle_circle(c1, r1, c2, r2, pick=-1):
    """One intersection point of two circles in the YZ plane."""
    dx, dy = c2[0] - c1[0], c2[1] - c1[1]
    d = math.hypot(dx, dy)
    a = (r1 * r1 - r2 * r2 + d * d) / (2.0 * d)
    h = math.sqrt(max(r1 * r1 - a * a, 0.0))
    mx, my = c1[0] + a * dx / d, c1[1] + a * dy / d
    return (mx - pick * h * dy / d, my + pick * h * dx / d)


def polar(p, length, ang_deg):
    t = math.radians(ang_deg)
    return (p[0] + length * math.cos(t), p[1] + length * math.sin(t))


def link(p0, p1, x0, holes):
    """Stadium plate from pivot p0 to pivot p1 (YZ), x in [x0, x0 + LINK_T],
    with pivot holes at the given YZ points."""
    cy, cz = (p0[0] + p1[0]) / 2.0, (p0[1] + p1[1]) / 2.0
    length = math.hypot(p1[0] - p0[0], p1[1] - p0[1])
    ang = math.degrees(math.atan2(p1[1] - p0[1], p1[0] - p0[0]))
    body = (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .center(cy, cz)
        .slot2D(length + 2 * LINK_R, 2 * LINK_R, ang)
        .extrude(LINK_T)
    )
    bores = (
        cq.Workplane("YZ", origin=(x0 - 1.0, 0, 0))
        .pushPoints(holes)
        .circle(HOLE_R)
        .extrude(LINK_T + 2.0)
    )
    return body.cut(bores).val()


def mechanism(x_inner, x_outer, theta_upper, lower_flipped):
    """The five links of one side for a given upper-arm angle."""
    up_tip = polar(TOP, L_LONG, theta_upper)
    up_hole = polar(TOP, L_HOLE, theta_upper)
    joint = circle_circle(MID, L_SHORT, up_hole, L_MID)
    # the lower arm is the same part; on one side it is mounted end-for-end
    lo_hole_dist = L_LONG - L_HOLE if lower_flipped else L_HOLE
    lo_hole = circle_circle(BOT, lo_hole_dist, joint, L_MID)
    theta_lo = math.degrees(math.atan2(lo_hole[1] - BOT[1], lo_hole[0] - BOT[0]))
    lo_tip = polar(BOT, L_LONG, theta_lo)
    return [
        link(TOP, up_tip, x_inner, [TOP, up_hole, up_tip]),      # upper arm
        link(BOT, lo_tip, x_inner, [BOT, lo_hole, lo_tip]),      # lower arm
        link(MID, joint, x_inner, [MID, joint]),                 # rocker
        link(up_hole, joint, x_outer, [up_hole, joint]),         # coupler 1
        link(joint, lo_hole, x_outer, [joint, lo_hole]),         # coupler 2
    ]


# --- box: rectangular tube with the three pivot bores through both walls ---
box = cq.Workplane("XY").box(BOX_W, BOX_D, BOX_H)
box = box.cut(
    cq.Workplane("XY").box(BOX_W - 2 * WALL, BOX_D + 2.0, BOX_H - 2 * WALL)
)
box = box.cut(
    cq.Workplane("YZ", origin=(-BOX_W / 2 - 1.0, 0, 0))
    .pushPoints([TOP, MID, BOT])
    .circle(HOLE_R)
    .extrude(BOX_W + 2.0)
)

bodies = [box.val()]
bodies += mechanism(
    x_inner=BOX_W / 2.0,
    x_outer=BOX_W / 2.0 + LINK_T,
    theta_upper=THETA_POS_X,
    lower_flipped=False,
)
bodies += mechanism(
    x_inner=-BOX_W / 2.0 - LINK_T,
    x_outer=-BOX_W / 2.0 - 2.0 * LINK_T,
    theta_upper=THETA_NEG_X,
    lower_flipped=True,
)

result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(bodies)])

VIEW = {"azimuth": 45, "elevation": 26}
